"""Articulated bone-like link: a curved, lofted shaft with a ball joint at the lower end and a
knuckle (hinge) head at the upper end.  The head carries a clevis slot that is open at the top and
cut right through at its leading end; the ball carries a slot open at the bottom whose ceiling ramps
up at 45 deg toward the trailing side.  Both slots have a pair of facing snap bumps on their walls."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BALL_R = 11.75                      # lower ball joint radius
BALL_C = (0.0, 0.0, 0.0)            # lower ball centre

HEAD_C = (13.2, 22.85, 98.45)       # upper (hinge) head centre
HEAD_R = 8.4                        # head knuckle radius (round about the pin axis)
HEAD_HALF_L = 3.25                  # half length of the knuckle's straight part along the pin

# shaft sections (horizontal ellipses): (z, cx, cy, a, b, major-axis angle deg)
SHAFT = [
    (-2.0, 0.5, 1.5, 9.0, 9.0, 0.0),
    (6.0, 1.75, 3.05, 9.05, 8.75, 90.0),
    (12.0, 2.7, 3.3, 10.2, 8.45, 90.0),
    (18.0, 3.7, 6.0, 9.55, 8.65, 70.0),
    (30.0, 4.50, 8.11, 10.13, 8.58, 57.1),
    (50.0, 6.19, 11.03, 9.79, 9.0, 35.1),
    (70.0, 8.12, 15.10, 9.07, 8.41, 34.6),
    (82.0, 9.85, 17.95, 9.22, 8.37, 141.8),
    (90.0, 11.7, 20.3, 10.0, 9.1, 150.0),
    (100.0, 13.2, 22.85, 11.4, 8.2, 149.6),
]
HEAD_FILLET = 0.0                   # blend between shaft and head
BALL_FILLET = 5.5                   # blend between shaft and ball

# upper hinge slot: open at the top and cut right through at the +s end
TOP_SLOT_W = 6.6
TOP_SLOT_ANG = 59.6                 # slot direction in XY (deg from +X)
TOP_TILT = 0.0                     # lean of local axis toward slot dir (tan)
TOP_PIN = (-1.2, 1.05)              # pin (bump) centre rel. head centre (along slot, along local axis)
TOP_FLOOR = -2.05                   # floor, rel. pin, along local axis
TOP_OPEN_S = 5.5                    # beyond this (rel. pin, along slot) the slot is cut right through
TOP_OPEN_LO = -8.75                 # depth of that open end rel. pin

# lower ball slot: open at the bottom, ceiling ramps up at 45 deg toward the -s end
BOT_SLOT_W = 7.15
BOT_SLOT_ANG = 25.7
BOT_TILT = 0.0
BOT_PIN = (0.0, -2.5, -1.2)         # pin centre rel. ball centre (along slot, along axis, along pin)
BOT_CEIL = 2.0                      # flat ceiling rel. pin
BOT_RAMP_S = -2.5                   # ramp starts here (rel. pin, along slot)

# snap bumps on the slot walls
BUMP_BASE_R = 3.2
BUMP_H = 1.75


def V(*a):
    return cq.Vector(*a)


def frame(ang_deg, tilt):
    """return (s, a, n): slot direction, local up axis, pin axis"""
    ang = math.radians(ang_deg)
    sh = V(math.cos(ang), math.sin(ang), 0)
    n = V(math.sin(ang), -math.cos(ang), 0)
    a = (sh * tilt + V(0, 0, 1)).normalized()
    s = a.cross(n).normalized()
    return s, a, n


def section(z, cx, cy, a, b, ang):
    """horizontal ellipse (major a along ang deg), parametrised to start near its +Y side (aligned loft seam)"""
    c = V(cx, cy, z)
    t0 = 90.0 - ang
    if abs(a - b) < 1e-6:
        e = cq.Edge.makeCircle(a, c, V(0, 0, 1), angle1=90, angle2=450)
    else:
        xd = V(math.cos(math.radians(ang)), math.sin(math.radians(ang)), 0)
        e = cq.Edge.makeEllipse(a, b, c, V(0, 0, 1), xd, angle1=t0, angle2=t0 + 360)
    return cq.Wire.assembleEdges([e])


def capsule(center, axis, side, r, half_l):
    """knuckle: cylinder of radius r along axis with hemispherical ends"""
    pl = cq.Plane(origin=V(*center), xDir=axis, normal=side.cross(axis) * -1)
    return (
        cq.Workplane(pl)
        .moveTo(-half_l - r, 0)
        .threePointArc((-half_l - r * math.cos(math.pi / 4), r * math.sin(math.pi / 4)), (-half_l, r))
        .lineTo(half_l, r)
        .threePointArc((half_l + r * math.cos(math.pi / 4), r * math.sin(math.pi / 4)), (half_l + r, 0))
        .close()
        .revolve(360, (-half_l - r, 0, 0), (half_l + r, 0, 0))
        .val()
    )


def local_frame(center, ang, tilt, ds=0.0, da=0.0, dn=0.0):
    s, a, n = frame(ang, tilt)
    o = V(*center) + s * ds + a * da + n * dn
    return o, s, a, n


def profile_cutter(origin, s, n, width, pts):
    """prism: closed polygon pts given in the (slot, local-axis) plane, extruded symmetrically along the pin"""
    pl = cq.Plane(origin=origin, xDir=s, normal=n)
    return cq.Workplane(pl).polyline(pts).close().extrude(width / 2.0, both=True)


def bumps(origin, n, width):
    rs = (BUMP_BASE_R ** 2 + BUMP_H ** 2) / (2 * BUMP_H)
    off = width / 2.0 + rs - BUMP_H
    b1 = cq.Solid.makeSphere(rs, origin + n * off, angleDegrees1=-90, angleDegrees2=90)
    b2 = cq.Solid.makeSphere(rs, origin - n * off, angleDegrees1=-90, angleDegrees2=90)
    return cq.Workplane().add(b1).union(cq.Workplane().add(b2))


# ---------------- body ----------------
shaft = cq.Solid.makeLoft([section(*s) for s in SHAFT])
ball = cq.Solid.makeSphere(BALL_R, V(*BALL_C), angleDegrees1=-90, angleDegrees2=90)
ball = ball.rotate(V(*BALL_C), V(*BALL_C) + V(0, 0, 1), BOT_SLOT_ANG + 180.0)   # seam inside the slot
hang = math.radians(TOP_SLOT_ANG)
h_n = V(math.sin(hang), -math.cos(hang), 0)        # pin axis (horizontal)
h_s = V(math.cos(hang), math.sin(hang), 0)         # slot direction
head = capsule(HEAD_C, h_n, h_s, HEAD_R, HEAD_HALF_L)

body = shaft.fuse(head)
hc = V(*HEAD_C)
head_edges = [e for e in body.Edges() if (e.Center() - hc).Length < 16 and e.Center().z < HEAD_C[2] + 1]
if HEAD_FILLET > 0 and head_edges:
    body = body.fillet(HEAD_FILLET, head_edges)
body = body.fuse(ball)
bc = V(*BALL_C)
ball_edges = [e for e in body.Edges() if (e.Center() - bc).Length < BALL_R + 3 and e.Center().z > bc.z]
if BALL_FILLET > 0 and ball_edges:
    body = body.fillet(BALL_FILLET, ball_edges)
body = cq.Workplane().add(body)

# ---------------- slots ----------------
BIG = 40.0
pt, st, at, nt = local_frame(HEAD_C, TOP_SLOT_ANG, TOP_TILT, TOP_PIN[0], TOP_PIN[1])
top_cut = profile_cutter(pt, st, nt, TOP_SLOT_W, [
    (-BIG, TOP_FLOOR), (TOP_OPEN_S, TOP_FLOOR), (TOP_OPEN_S, TOP_OPEN_LO),
    (BIG, TOP_OPEN_LO), (BIG, BIG), (-BIG, BIG)])
body = body.cut(top_cut)

pb, sb, ab, nb = local_frame(BALL_C, BOT_SLOT_ANG, BOT_TILT, BOT_PIN[0], BOT_PIN[1], BOT_PIN[2])
ramp_top = BOT_CEIL + (BOT_RAMP_S + 20.0)
bot_cut = profile_cutter(pb, sb, nb, BOT_SLOT_W, [
    (-20.0, -BIG), (BIG, -BIG), (BIG, BOT_CEIL), (BOT_RAMP_S, BOT_CEIL), (-20.0, ramp_top)])
body = body.cut(bot_cut)

body = body.union(bumps(pt, nt, TOP_SLOT_W))
body = body.union(bumps(pb, nb, BOT_SLOT_W))

result = body
VIEW = {"azimuth": 45, "elevation": 26}
